import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H_TOTAL = 7260.0          # overall pole height incl. cap
POLE_R = 143.0            # pole radius
CAP_R = 150.0             # pole cap radius (slightly proud of the pole)
CAP_H = 16.0              # cap cylindrical height
CAP_CONE = 45.0           # cap cone rise
H_POLE = H_TOTAL - CAP_H - CAP_CONE

# cross arms (three, on the +Y side of the pole)
ARM_L = 1620.0
ARM_W = 83.0              # along Y
ARM_T = 104.0             # along Z
ARM_Y0 = 96.0             # front face of arm (Y)
ARM_FILLET = 8.0
ARM_Z = [6808.0, 6117.0, 5431.0]   # arm centre heights

# pin insulators
INS_X = [-674.0, -368.0, 368.0, 674.0]
INS_BODY_R = 71.0
INS_BODY_H = 170.0
INS_LIP_R = 78.0
INS_LIP_H = 18.0
INS_NECK_R = 52.0
INS_NECK_H = 24.0
INS_HEAD_R = 64.0
INS_HEAD_H = 52.0
INS_DOME = 4.0           # small chamfer at the top of the head
INS_SEAT_R = 33.0
INS_SLOT_D = 20.0
INS_SLOT_W = 20.0

# clamp collars (plates around the pole, reaching back to the arm)
COL_HX = 159.0            # half width in X
COL_FRONT = 169.0         # reach in -Y
COL_STRAIGHT = -55.0      # Y where straight sides end and the rounded front begins
COL_T = 36.0              # plate thickness
COL_DZ = -8.0             # collar centre relative to arm centre

# through bolts with hex nuts on the back of the arm
BOLT_X = 171.0
NUT_AF = 58.0
NUT_L = 36.0
BOLT_R = 12.0
BOLT_STICK = 6.0

# wood checks (cracks) in the pole
CHECK_W = 22.0
CHECK_DEPTH = 16.0
GROOVE_W = 46.0
GROOVE_DEPTH = 6.0
CRACK_W = 4.0
CRACK_DEPTH = 14.0
CRACK_ANGLE = -130.0
POLE_SEAM_ANGLE = 130.0


def pole():
    # seam of the turned pole placed at the back, where a check runs anyway
    body = (cq.Workplane("XY").circle(POLE_R).extrude(H_POLE)
            .rotate((0, 0, 0), (0, 0, 1), POLE_SEAM_ANGLE))
    cap = (
        cq.Workplane("XZ")
        .polyline([(0, H_POLE - 1.0), (CAP_R, H_POLE - 1.0), (CAP_R, H_POLE + CAP_H),
                   (0, H_POLE + CAP_H + CAP_CONE)])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), CRACK_ANGLE)
    )
    return body.union(cap)


def arm(zc):
    return (
        cq.Workplane("XY")
        .box(ARM_L, ARM_W, ARM_T)
        .edges()
        .fillet(ARM_FILLET)
        .translate((0, ARM_Y0 + ARM_W / 2.0, zc))
    )


def insulator(x, y, z0):
    z1 = INS_BODY_H
    z2 = z1 + INS_LIP_H
    z3 = z2 + INS_NECK_H
    z4 = z3 + INS_HEAD_H
    pts = [
        (0, 0), (INS_BODY_R, 0), (INS_BODY_R, z1), (INS_LIP_R, z1),
        (INS_LIP_R, z2), (INS_NECK_R, z2), (INS_NECK_R, z3),
        (INS_HEAD_R, z3), (INS_HEAD_R, z4 - INS_DOME),
        (INS_HEAD_R - INS_DOME, z4), (0, z4),
    ]
    ins = cq.Workplane("XZ").polyline(pts).close().revolve(360, (0, 0, 0), (0, 1, 0))
    # wire saddle: narrow slot across the head (along Y) with a round seat in the middle
    slot_len = 2.0 * (INS_HEAD_R - 8.0)
    slot = (
        cq.Workplane("XY", origin=(0, 0, z4 - INS_SLOT_D))
        .slot2D(slot_len, INS_SLOT_W, 90)
        .extrude(INS_SLOT_D + 5.0)
    )
    seat = cq.Workplane("XY").sphere(INS_SEAT_R).translate((0, 0, z4 + INS_SEAT_R * 0.25))
    ins = ins.cut(slot).cut(seat)
    return ins.translate((x, y, z0))


def collar(zc):
    y_back = ARM_Y0 + 2.0
    side = (
        cq.Workplane("XY")
        .center(0, (y_back + COL_STRAIGHT) / 2.0)
        .rect(2 * COL_HX, y_back - COL_STRAIGHT)
        .extrude(COL_T)
    )
    front = (
        cq.Workplane("XY")
        .center(0, COL_STRAIGHT)
        .ellipse(COL_HX, COL_FRONT + COL_STRAIGHT)
        .extrude(COL_T)
    )
    plate = side.union(front)
    return plate.translate((0, 0, zc - COL_T / 2.0))


def bolts(zc):
    y_back = ARM_Y0 + ARM_W
    out = None
    for sx in (-1, 1):
        nut = (
            cq.Workplane("XZ", origin=(sx * BOLT_X, y_back, zc))
            .polygon(6, NUT_AF / math.cos(math.pi / 6))
            .extrude(-NUT_L)
        )
        rod = (
            cq.Workplane("XZ", origin=(sx * BOLT_X, y_back - 10.0, zc))
            .circle(BOLT_R)
            .extrude(-(NUT_L + BOLT_STICK + 10.0))
        )
        piece = nut.union(rod)
        out = piece if out is None else out.union(piece)
    return out


def check(theta_deg, z0, z1, width=CHECK_W, depth=CHECK_DEPTH, round_ends=True):
    length = z1 - z0
    c = cq.Workplane("XY").box(depth * 2.0, width, length)
    if round_ends:
        c = c.edges("|X").fillet(width * 0.49)
    return c.translate((POLE_R, 0, z0 + length / 2.0)).rotate(
        (0, 0, 0), (0, 0, 1), theta_deg)


result = pole()

# checks / grooves in the wooden pole (cut before hardware is attached)
cuts = [
    check(-81.0, 40.0, H_POLE - 40.0, GROOVE_W, GROOVE_DEPTH, False),
    check(-4.0, 6700.0, H_POLE - 5.0),
    check(-50.0, 480.0, 4670.0),
    check(-4.0, 1640.0, 5620.0),
    check(103.0, 700.0, 5560.0),
]
for c in cuts:
    result = result.cut(c)

# radial crack in the conical top of the cap (from the centre out to the rim),
# its floor follows the cone slope at a constant depth
z_apex = H_POLE + CAP_H + CAP_CONE
z_rim = H_POLE + CAP_H
slope = CAP_CONE / CAP_R
r_out = CAP_R + 10.0
crack = (
    cq.Workplane("XZ", origin=(0, CRACK_W / 2.0, 0))
    .polyline([
        (-2.0, z_apex + 10.0),
        (r_out, z_rim + 10.0),
        (r_out, z_rim - slope * 10.0 - CRACK_DEPTH),
        (-2.0, z_apex - CRACK_DEPTH),
    ])
    .close()
    .extrude(CRACK_W)
    .rotate((0, 0, 0), (0, 0, 1), CRACK_ANGLE)
)
result = result.cut(crack)

for zc in ARM_Z:
    result = result.union(arm(zc))
    for x in INS_X:
        result = result.union(insulator(x, ARM_Y0 + ARM_W / 2.0, zc + ARM_T / 2.0 - 1.0))
    result = result.union(collar(zc + COL_DZ))
    result = result.union(bolts(zc - 10.0))

VIEW = {"azimuth": 45, "elevation": 26}
